import math
import cadquery as cq

# =====================================================================
#  Wheel with balloon tyre (axis = Y, keyed hub face towards -Y)
# =====================================================================

# ---------------------------------------------------------------- tyre
R_OUT = 150.0        # tyre outer radius (crown centre)
HALF_W = 64.0        # half tyre width (flat side walls at y = +-HALF_W)
R_SH = 111.0         # radius of the shoulder corner (side wall -> crown)
R_RIM = 78.0         # rim / tyre boundary radius
BEAD_Y = 50.0        # |y| of the tyre bead (side wall slopes in to the rim)
SW_BULGE = 1.5       # outward bulge of the side wall

# ---------------------------------------------------------------- rim / dish
LIP_Y = BEAD_Y       # rim edge plane (|y|), at the tyre bead
LIP_R = 72.0         # inner radius of the (slightly sloped) rim lip
# dish profiles (radius, depth below the rim edge) from the lip to the well
F_DISH = ((LIP_R, 2.5), (67.7, 5.5), (64.3, 10.0), (60.8, 14.0), (56.5, 17.5), (53.0, 20.5),
          (51.5, 24.5))
B_DISH = ((LIP_R, 2.5), (67.7, 5.5), (63.0, 10.5), (58.0, 15.0), (53.5, 17.8), (51.5, 19.0))
WELL_R = 51.5        # well radius (= last dish point)
WELL_BOT = -9.5      # front well bottom ring (y)
F_DISC_Y = -8.0      # front hub disc face
DISC_R = 48.0
B_DISC_Y = 31.0      # back hub face (= LIP_Y - last B_DISH depth)

# ---------------------------------------------------------------- hub (front)
BORE_R = 16.0
BORE_D = 25.0
KEY_W = 6.0
KEY_D = 4.0
KEY_ANG = 135.0
SLOT_RC = 35.0       # kidney slot centre-line radius
SLOT_W = 13.5
SLOT_SPAN = 46.0     # deg
SLOT_ANGS = (79.0, 199.0, 319.0)
SLOT_DEPTH = 9.0
PAD_RC = 40.5        # square bolt pockets
PAD_S = 12.5
PAD_DEPTH = 3.0
PAD_HOLE_R = 2.8
PAD_ANGS = (19.5, 139.5, 259.5)

# ---------------------------------------------------------------- hub (back)
TRI_R = 43.0         # triangle (groove outline) circumradius
TRI_ANG = 27.0       # angle of the first triangle corner
TRI_FILLET = 5.0
TRI_GROOVE = 3.5     # width of the triangular groove
TRI_DEPTH = 3.0
BSLOT_L = 40.0
BSLOT_W = 4.0
BSLOT_OFF = 33.0     # distance of back slot centres from the axis
BSLOT_DEPTH = 3.0

# ---------------------------------------------------------------- tread
N_PITCH = 15         # long/short groove pairs per side
PITCH = 360.0 / N_PITCH
G_W = 3.5            # groove width
G_D = 2.5            # groove depth
G_UP = 3.0           # tool height above the surface
G_DPHI = 11.0        # circumferential sweep of a long groove (deg)
G_EXP = 2.5          # shape exponent of the groove curve
G_LONG_END = 1.0     # axial end (y) of a long groove
G_SHORT_END = -30.0  # axial end (y) of a short groove
G_START_Y = -63.0    # start of the crown part of a groove (shoulder)
G_RUNOUT = 6.0       # run-out of the groove arc over the shoulder (deg)
G_SIDE_END = 107.0   # grooves continue down the side wall to this radius
G_SIDE_OUT = 115.0
PHI0 = 3.0           # angular position of the first long front groove
PH_FS = 11.0         # phase of front short grooves (rel. to front long)
PH_BL = 10.0         # phase of back long grooves
PH_BS = -2.0         # phase of back short grooves

SEAM_TYRE = 110.0    # rotates the tyre revolve seam to phi = 250 deg (hidden side)
SEAM_RIM = -90.0     # rotates the rim revolve seam to phi = 90 deg (hidden in 3/4 views)

# crown arc: centre radius and radius (through shoulder corners and crown)
CR_C = (R_OUT ** 2 - R_SH ** 2 - HALF_W ** 2) / (2.0 * (R_OUT - R_SH))
CR_R = R_OUT - CR_C


def crown_r(y):
    return CR_C + math.sqrt(max(CR_R ** 2 - y ** 2, 0.0))


def crown_n(y, phi):
    """outward unit normal of the crown surface"""
    nr = (crown_r(y) - CR_C) / CR_R
    ny = y / CR_R
    a = math.radians(phi)
    return cq.Vector(nr * math.cos(a), ny, nr * math.sin(a))


def P(r, y, phi):
    a = math.radians(phi)
    return cq.Vector(r * math.cos(a), y, r * math.sin(a))


def groove_phi(y):
    t = (y + HALF_W) / (G_LONG_END + HALF_W)
    return G_DPHI * max(t, 0.0) ** G_EXP


def groove_pt(y):
    return P(crown_r(y), y, groove_phi(y))


# ---------------------------------------------------------------- tyre body
tyre = (
    cq.Workplane("XY")
    .moveTo(R_RIM, -BEAD_Y)
    .threePointArc((0.5 * (R_RIM + R_SH), -0.5 * (BEAD_Y + HALF_W) - SW_BULGE), (R_SH, -HALF_W))
    .threePointArc((R_OUT, 0), (R_SH, HALF_W))
    .threePointArc((0.5 * (R_RIM + R_SH), 0.5 * (BEAD_Y + HALF_W) + SW_BULGE), (R_RIM, BEAD_Y))
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), SEAM_TYRE)
)


# ---------------------------------------------------------------- groove tools
def groove_tool(y_end):
    """rectangular groove (G_W x G_D) following the crown on a circular arc
    from the shoulder to y_end; the arc is continued backwards over the
    shoulder (run-out) and the crown end is rounded"""
    A = groove_pt(G_START_Y)
    B = groove_pt(y_end)
    M = groove_pt(0.5 * (G_START_Y + y_end))
    a = A - B
    b = M - B
    axb = a.cross(b)
    C = B + (b * a.dot(a) - a * b.dot(b)).cross(axb) * (1.0 / (2.0 * axb.dot(axb)))
    rho = (A - C).Length
    n = (A - C).cross(M - C).normalized()
    u0 = (A - C).normalized()
    v0 = n.cross(u0)
    ang = math.degrees(math.atan2((B - C).dot(v0), (B - C).dot(u0)))
    if ang < 0:
        ang += 360.0
    bk = math.radians(G_RUNOUT)
    u = u0 * math.cos(bk) - v0 * math.sin(bk)
    A2 = C + u * rho
    hw = G_W / 2.0
    rect = cq.Wire.makePolygon(
        [A2 + u * h + n * w for (h, w) in ((-G_D, -hw), (-G_D, hw), (G_UP, hw), (G_UP, -hw))],
        close=True,
    )
    tube = cq.Solid.revolve(rect, [], ang + G_RUNOUT, C, C + n)
    uB = (B - C).normalized()
    cap = cq.Solid.makeCylinder(hw, G_D + G_UP, B - uB * G_D, uB)
    return tube.fuse(cap).clean()


def circle3(p1, p2, p3):
    """centre and radius of the 2D circle through three points"""
    ax, ay = p1
    bx, by = p2
    cx, cy = p3
    d = 2.0 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay)
          + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx)
          + (cx * cx + cy * cy) * (bx - ax)) / d
    return ux, uy, math.hypot(ax - ux, ay - uy)


def side_tool():
    """short round-ended slot carrying a groove over the shoulder down the
    front side wall to radius G_SIDE_END"""
    mid = (0.5 * (R_RIM + R_SH), -0.5 * (BEAD_Y + HALF_W) - SW_BULGE)
    cx, cy, rr = circle3((R_RIM, -BEAD_Y), mid, (R_SH, -HALF_W))
    rm = 0.5 * (G_SIDE_END + G_SIDE_OUT)
    pm = cq.Vector(rm, cy - math.sqrt(rr ** 2 - (rm - cx) ** 2), 0)
    n_out = cq.Vector(pm.x - cx, pm.y - cy, 0).normalized()
    d = cq.Vector(-n_out.y, n_out.x, 0)
    plane = cq.Plane(origin=pm - n_out * G_D, xDir=d, normal=n_out)
    return (
        cq.Workplane(plane)
        .slot2D(G_SIDE_OUT - G_SIDE_END + G_W, G_W)
        .extrude(G_D + G_UP)
        .val()
    )


long_t = groove_tool(G_LONG_END)
short_t = groove_tool(G_SHORT_END)
side_t = side_tool()
long_b = long_t.mirror("XZ")
short_b = short_t.mirror("XZ")
side_b = side_t.mirror("XZ")

Y0 = cq.Vector(0, 0, 0)
Y1 = cq.Vector(0, 1, 0)
tools = []
for k in range(N_PITCH):
    base = PHI0 + k * PITCH
    for tool, side, ph in (
        (long_t, side_t, base),
        (short_t, side_t, base + PH_FS),
        (long_b, side_b, base + PH_BL),
        (short_b, side_b, base + PH_BS),
    ):
        tools.append(tool.rotate(Y0, Y1, -ph))
        tools.append(side.rotate(Y0, Y1, -ph))

tyre_s = tyre.val().cut(*tools)

# ---------------------------------------------------------------- rim body
def prof(pts, sgn):
    return [(r, sgn * (LIP_Y - d)) for (r, d) in pts]


f_dish = prof(F_DISH, -1)
b_dish = prof(B_DISH, 1)
tf = (F_DISH[1][0] - F_DISH[0][0], F_DISH[1][1] - F_DISH[0][1])
tb = (B_DISH[1][0] - B_DISH[0][0], B_DISH[1][1] - B_DISH[0][1])
rim = (
    cq.Workplane("XY")
    .moveTo(0, F_DISC_Y)
    .lineTo(DISC_R, F_DISC_Y)
    .lineTo(DISC_R + 1.5, WELL_BOT)
    .lineTo(WELL_R, WELL_BOT)
    .lineTo(*f_dish[-1])
    .spline(f_dish[::-1][1:], tangents=[(0, -1), (-tf[0], tf[1])], includeCurrent=True)
    .lineTo(R_RIM, -LIP_Y)
    .lineTo(R_RIM, LIP_Y)
    .lineTo(*b_dish[0])
    .spline(b_dish[1:], tangents=[(tb[0], -tb[1]), (0, -1)], includeCurrent=True)
    .lineTo(0, B_DISC_Y)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), SEAM_RIM)
)

# ---------------------------------------------------------------- front hub features
# work plane on the front disc face, local x = +X, local y = +Z, normal = -Y
fplane = cq.Plane(origin=(0, F_DISC_Y, 0), xDir=(1, 0, 0), normal=(0, -1, 0))


def fpt(r, ang):
    a = math.radians(ang)
    return (r * math.cos(a), r * math.sin(a))


bore = cq.Workplane(fplane).circle(BORE_R).extrude(-BORE_D)
key = (
    cq.Workplane(fplane)
    .center(*fpt(BORE_R, KEY_ANG))
    .transformed(rotate=(0, 0, KEY_ANG))
    .rect(2 * KEY_D, KEY_W)
    .extrude(-BORE_D)
)
rim = rim.cut(bore).cut(key)


def kidney(a):
    a1 = a - SLOT_SPAN / 2
    a2 = a + SLOT_SPAN / 2
    ro = SLOT_RC + SLOT_W / 2
    ri = SLOT_RC - SLOT_W / 2

    def cap_mid(ang, sgn):
        c = fpt(SLOT_RC, ang)
        t = math.radians(ang + 90 * sgn)
        return (c[0] + SLOT_W / 2 * math.cos(t), c[1] + SLOT_W / 2 * math.sin(t))

    return (
        cq.Workplane(fplane)
        .moveTo(*fpt(ro, a1))
        .threePointArc(fpt(ro, a), fpt(ro, a2))
        .threePointArc(cap_mid(a2, 1), fpt(ri, a2))
        .threePointArc(fpt(ri, a), fpt(ri, a1))
        .threePointArc(cap_mid(a1, -1), fpt(ro, a1))
        .close()
        .extrude(-SLOT_DEPTH)
    )


for a in SLOT_ANGS:
    rim = rim.cut(kidney(a))

for a in PAD_ANGS:
    c = fpt(PAD_RC, a)
    pk = (
        cq.Workplane(fplane)
        .center(*c)
        .transformed(rotate=(0, 0, a))
        .rect(PAD_S, PAD_S)
        .extrude(-PAD_DEPTH)
    )
    hole = cq.Workplane(fplane).center(*c).circle(PAD_HOLE_R).extrude(-30)
    rim = rim.cut(pk).cut(hole)

# ---------------------------------------------------------------- back hub features
# plane on the back disc face: local x = -X, local y = +Z, normal = +Y
bplane = cq.Plane(origin=(0, B_DISC_Y, 0), xDir=(-1, 0, 0), normal=(0, 1, 0))


def bpt(r, ang):
    a = math.radians(ang)
    return (-r * math.cos(a), r * math.sin(a))


TRI_ANGS = [TRI_ANG + 120.0 * i for i in range(3)]
tri_out = (
    cq.Workplane(bplane)
    .polyline([bpt(TRI_R, a) for a in TRI_ANGS]).close()
    .extrude(-TRI_DEPTH)
    .edges("|Y").fillet(TRI_FILLET)
)
r_in = TRI_R - 2.0 * TRI_GROOVE
tri_in = (
    cq.Workplane(bplane)
    .polyline([bpt(r_in, a) for a in TRI_ANGS]).close()
    .extrude(-TRI_DEPTH)
    .edges("|Y").fillet(max(TRI_FILLET - TRI_GROOVE, 0.8))
)
rim = rim.cut(tri_out.cut(tri_in))

for a in TRI_ANGS:
    am = a + 60.0
    c = bpt(BSLOT_OFF, am)
    bs = (
        cq.Workplane(bplane)
        .center(*c)
        .transformed(rotate=(0, 0, 90.0 - am))
        .slot2D(BSLOT_L, BSLOT_W)
        .extrude(-BSLOT_DEPTH)
    )
    rim = rim.cut(bs)

result = cq.Workplane("XY").add(tyre_s.fuse(rim.val()).clean())
